import math
import cadquery as cq

# camera used for the preview render (default iso view)
VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
BODY_W = 40.0          # width along X
BODY_STRAIGHT = 10.0   # straight part of the D footprint (front face -> arc centre)
BODY_H = 30.0          # height along Z
TOP_R = 13.0           # rounding of the top edges (sides + back)

HOLE_Y = 16.3          # bottom (threaded) hole position behind the front face
HOLE_D = 20.0          # plain bore (thread left out)
HOLE_CH = 0.7          # chamfer at the mouth
HOLE_DEPTH = 20.0      # depth of the cylindrical part
DRILL_ANGLE = 118.0    # drill point

# hook (snap tongue) on the front face, profile measured forward from face (-Y)
HOOK_HALF_W = 10.8     # half width of the hook plate
HOOK_TOP = 24.1        # top of the hook
HOOK_UNDER = 14.2      # underside of the overhanging top part
HOOK_FRONT = 11.7      # front face of the hanging leg
HOOK_ARC_R = 8.2       # outer rounding of hook
LEG_INNER = 8.4        # inner face of leg (upper part)
BARB_TOP_Z = 9.6       # top of barb
BARB_INNER_TOP = 7.6   # barb inner face at top
BARB_INNER_BOT = 8.5   # barb inner face at bottom

# rail "ears" either side of the hook top
EAR_HALF_W = 14.5
EAR_DEPTH = 6.7
EAR_CH_D = 4.1         # lower front chamfer of the ear (depth)
EAR_CH_Z = 4.7         # lower front chamfer of the ear (height)
EAR_CH_FILLET = 2.0    # small round between ear front and its chamfer
EAR_DOVE_Z = 18.2      # height where the dovetail chamfer meets the ear end

# ---------------- body: D-shaped block with rounded top ----------------
R = BODY_W / 2.0
body = (
    cq.Workplane("XY")
    .moveTo(-R, 0)
    .lineTo(R, 0)
    .lineTo(R, BODY_STRAIGHT)
    .threePointArc((0, BODY_STRAIGHT + R), (-R, BODY_STRAIGHT))
    .close()
    .extrude(BODY_H)
)
# round every top edge except the flat front one
body = body.edges(cq.selectors.BoxSelector(
    (-R - 1, 0.5, BODY_H - 0.1), (R + 1, BODY_STRAIGHT + R + 1, BODY_H + 0.1))).fillet(TOP_R)

# blind bottom hole (thread omitted) with drill point and small mouth chamfer
tip = (HOLE_D / 2.0) / math.tan(math.radians(DRILL_ANGLE / 2.0))
hole = (
    cq.Workplane("XZ", origin=(0, HOLE_Y, 0))
    .polyline([
        (0, -1),
        (HOLE_D / 2.0 + HOLE_CH + 1, -1),
        (HOLE_D / 2.0 + HOLE_CH + 1, 0),
        (HOLE_D / 2.0 + HOLE_CH, 0),
        (HOLE_D / 2.0, HOLE_CH),
        (HOLE_D / 2.0, HOLE_DEPTH),
        (0, HOLE_DEPTH + tip),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(hole)

# ---------------- hook (snap tongue) ----------------
# L-shaped profile in a YZ plane; local x = world Y (negative = forward), local y = Z
arc_cz = HOOK_TOP - HOOK_ARC_R
arc_cy = -(HOOK_FRONT - HOOK_ARC_R)
a45 = math.radians(45)
arc_mid = (arc_cy - HOOK_ARC_R * math.cos(a45), arc_cz + HOOK_ARC_R * math.sin(a45))

hook = (
    cq.Workplane("YZ", origin=(-EAR_HALF_W, 0, 0))
    .moveTo(0, HOOK_UNDER)
    .lineTo(-LEG_INNER, HOOK_UNDER)
    .lineTo(-LEG_INNER, BARB_TOP_Z)
    .lineTo(-BARB_INNER_TOP, BARB_TOP_Z)
    .lineTo(-BARB_INNER_BOT, 0)
    .lineTo(-HOOK_FRONT, 0)
    .lineTo(-HOOK_FRONT, arc_cz)
    .threePointArc(arc_mid, (arc_cy, HOOK_TOP))
    .lineTo(0, HOOK_TOP)
    .close()
    .extrude(2 * EAR_HALF_W)
)

# outside the plate width only the short "ears" of the tongue remain
BIG = 50.0
for s in (1, -1):
    xo = s * (HOOK_HALF_W + BIG / 2.0)
    # remove everything in front of the ear face
    hook = hook.cut(cq.Workplane("XY").box(BIG, BIG, BIG).translate((xo, -EAR_DEPTH - BIG / 2.0, BIG / 2.0 - 1)))
    # remove the hanging leg
    hook = hook.cut(cq.Workplane("XY").box(BIG, BIG, BIG).translate((xo, 0, HOOK_UNDER - BIG / 2.0)))
    # lower front chamfer of the ear
    x0 = HOOK_HALF_W if s > 0 else -EAR_HALF_W - 1
    tri = (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .polyline([(-(EAR_DEPTH - EAR_CH_D), HOOK_UNDER - 0.01),
                   (-EAR_DEPTH - 0.01, HOOK_UNDER + EAR_CH_Z + 0.01 * EAR_CH_Z / EAR_CH_D),
                   (-EAR_DEPTH - 1, HOOK_UNDER - 1)])
        .close()
        .extrude(EAR_HALF_W - HOOK_HALF_W + 1)
    )
    hook = hook.cut(tri)

# small round between the ear fronts and their chamfers
hook = hook.edges(cq.selectors.BoxSelector(
    (-EAR_HALF_W - 0.1, -EAR_DEPTH - 0.1, HOOK_UNDER + EAR_CH_Z - 0.1),
    (EAR_HALF_W + 0.1, -EAR_DEPTH + 0.1, HOOK_UNDER + EAR_CH_Z + 0.1))).fillet(EAR_CH_FILLET)

# dovetail chamfers under the ears
k = (EAR_DOVE_Z - HOOK_UNDER) / (EAR_HALF_W - HOOK_HALF_W)
for s in (1, -1):
    pts = [(HOOK_HALF_W, HOOK_UNDER), (EAR_HALF_W + 1, HOOK_UNDER + k * (EAR_HALF_W + 1 - HOOK_HALF_W)),
           (EAR_HALF_W + 1, HOOK_UNDER - 1), (HOOK_HALF_W, HOOK_UNDER - 1)]
    dv = (
        cq.Workplane("XZ")  # normal -Y: extrudes forward from the body face
        .polyline([(s * x, z) for x, z in pts])
        .close()
        .extrude(HOOK_FRONT + 2)
    )
    hook = hook.cut(dv)

result = body.union(hook).clean()
